import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 12.8            # overall plate height (wall top)
D = 7.3             # general pocket depth from the top
PAD_D = 4.0         # depth of the raised central pad below the top
T_OUT = 3.7         # outer wall thickness
RIB_MID = 3.25      # rib thickness between centre and side columns
RIB_SIDE = 3.7      # rib between outer strip and long side pocket
RIB_H = 3.5         # horizontal rib thickness

# outline
X_UP = 89.5         # half width of the upper (rear) section
X_LO = 114.5        # half width of the lower (front) section
Y_TOP = 118.35      # rear edge
Y_BOT = -118.5      # front edge of the side wings
Y_STEP_HI = 44.8    # where the 45 deg transition starts (at X_UP)
Y_STEP_LO = 20.4    # where it ends (at X_LO)
C_TOP = 4.5         # small chamfer on the two rear corners
X_NOTCH = 46.8      # half width of the recessed front centre
NOTCH = 20.7        # depth of the front recess (45 deg sides)

# internal layout
X_RIB_MID_IN = 46.8             # inner face of the centre ribs
X_RIB_SIDE_IN = X_UP - RIB_SIDE  # inner face of side rib (85.5)
Y_RIB_LO = 41.6                  # front face of the horizontal rib
PAD_BACK = 14.6                  # rear edge of the raised pad
LIP = 3.0                        # flat top width of the front lip of the centre pocket
SLOPE_W = 2.5                    # plan width of the slope from the lip down to the pad

# holes
D_SMALL = 5.6
D_UP_SMALL = 6.2
D_PAD_BIG = 19.0
D_UP_BIG = 11.5
D_UP_MED = 8.7
D_CB_THRU = 5.6
D_CB = 11.2
CB_DEPTH = 2.8
D_CSK = 11.5
SLOT_W = 5.3
SLOT_LEN = 56.0
SLOT_X = 58.0
SLOT_YC = -54.6
STRIP_X = 104.75
STRIP_Y = (-7.4, -107.4)
PAD_HX = 31.25
PAD_HY = (1.8, -78.4)
PAD_CY = -38.4
UP_HY = 91.6
UP_HX = (33.0, 62.5)
UP_BIG_Y = 80.4
UP_MED_Y = 104.1

# ---------------- outline ----------------
yf = Y_BOT + NOTCH
pts = [
    (-X_LO, Y_BOT),
    (-(X_NOTCH + NOTCH), Y_BOT),
    (-X_NOTCH, yf),
    (X_NOTCH, yf),
    (X_NOTCH + NOTCH, Y_BOT),
    (X_LO, Y_BOT),
    (X_LO, Y_STEP_LO),
    (X_UP, Y_STEP_HI),
    (X_UP, Y_TOP - C_TOP),
    (X_UP - C_TOP, Y_TOP),
    (-(X_UP - C_TOP), Y_TOP),
    (-X_UP, Y_TOP - C_TOP),
    (-X_UP, Y_STEP_HI),
    (-X_LO, Y_STEP_LO),
]

outline = cq.Workplane("XY").polyline(pts).close()
body = outline.extrude(H)

# inner region (outline offset inward by the wall thickness)
inner_wire = cq.Workplane("XY").polyline(pts).close().val()
inner_face = cq.Face.makeFromWires(inner_wire.offset2D(-T_OUT, "intersection")[0])
inner = cq.Workplane("XY").add(inner_face).wires().toPending().extrude(H)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


BIG = 500.0
z0 = H - D
cells = []
for s in (-1, 1):
    # outer strip column
    xa, xb = sorted((s * X_UP, s * BIG))
    cells.append(box(xa, xb, -BIG, BIG, z0, H + 1))
    # long side column, upper and lower
    xa, xb = sorted((s * X_RIB_SIDE_IN, s * (X_RIB_MID_IN + RIB_MID)))
    cells.append(box(xa, xb, Y_RIB_LO + RIB_H, BIG, z0, H + 1))
    cells.append(box(xa, xb, -BIG, Y_RIB_LO, z0, H + 1))
# centre column
cells.append(box(-X_RIB_MID_IN, X_RIB_MID_IN, Y_RIB_LO + RIB_H, BIG, z0, H + 1))
centre_lo = box(-X_RIB_MID_IN, X_RIB_MID_IN, yf + LIP, Y_RIB_LO, z0, H + 1)

pockets = centre_lo
for c in cells:
    pockets = pockets.union(c.intersect(inner))

body = body.cut(pockets)

# raised pad in the centre-front pocket
y_lip = yf + LIP
pad_prof = [
    (PAD_BACK, z0 - 0.01),
    (PAD_BACK, H - PAD_D),
    (y_lip + SLOPE_W, H - PAD_D),
    (y_lip, H),
    (y_lip - 0.5, H),
    (y_lip - 0.5, z0 - 0.01),
]
pad = (cq.Workplane("YZ", origin=(-X_RIB_MID_IN, 0, 0))
       .polyline(pad_prof).close()
       .extrude(2 * X_RIB_MID_IN))
body = body.union(pad)

# ---------------- holes ----------------
def cyl(x, y, d, z_lo=-1.0, z_hi=H + 1):
    return (cq.Workplane("XY").workplane(offset=z_lo)
            .center(x, y).circle(d / 2).extrude(z_hi - z_lo))


cutters = []
# plain through holes in the upper pockets
for hx in UP_HX:
    for s in (-1, 1):
        cutters.append(cyl(s * hx, UP_HY, D_UP_SMALL))
cutters.append(cyl(0, UP_BIG_Y, D_UP_BIG))
cutters.append(cyl(0, UP_MED_Y, D_UP_MED))
# pad holes
cutters.append(cyl(0, PAD_CY, D_PAD_BIG))
for s in (-1, 1):
    for hy in PAD_HY:
        cutters.append(cyl(s * PAD_HX, hy, D_SMALL))
        # countersink from below
        r_csk = D_CSK / 2 + 0.5   # 90 deg cone, started 0.5 below the bottom face
        cutters.append(cq.Workplane("XY").add(
            cq.Solid.makeCone(r_csk, 0, r_csk,
                              pnt=cq.Vector(s * PAD_HX, hy, -0.5),
                              dir=cq.Vector(0, 0, 1))))
# counterbored holes in the outer strips
for s in (-1, 1):
    for hy in STRIP_Y:
        cutters.append(cyl(s * STRIP_X, hy, D_CB_THRU))
        cutters.append(cyl(s * STRIP_X, hy, D_CB, z0 - CB_DEPTH, H + 1))
# slots
for s in (-1, 1):
    cutters.append(cq.Workplane("XY").workplane(offset=-1)
                   .center(s * SLOT_X, SLOT_YC)
                   .slot2D(SLOT_LEN, SLOT_W, angle=90).extrude(H + 2))

for c in cutters:
    body = body.cut(c)

result = body
